import cadquery as cq

# =====================================================================
# Cylindrical adapter: round body with a small top spigot, an axial
# through hole, a bottom bore, two bottom flats and a set-screw hole.
# Z is the axis, bottom face at Z = 0, the flats are normal to X.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
D_BODY = 24.0        # main cylinder diameter
H_BODY = 36.3        # main cylinder height
D_PIN = 8.0          # top spigot diameter
H_PIN = 9.7          # top spigot height
PIN_CHAMFER = 0.5    # chamfer on spigot top edge

ACROSS_FLATS = 17.7  # distance between the two bottom flats (normal to X)
H_FLAT = 7.3         # height of the flats from the bottom face

D_THRU = 3.3         # axial through hole
THRU_CHAMFER = 0.35  # countersink at spigot top

D_BORE = 8.5         # bottom bore
BORE_DEPTH = 12.0
BORE_CHAMFER = 0.3

D_CROSS = 2.0        # set-screw hole on the -X flat, into the bore
Z_CROSS = H_FLAT / 2.0

BOTTOM_CHAMFER = 0.4  # chamfer round the bottom face outline

SEAM_ANGLE = 45.0     # where the periodic seams of the round faces sit (deg about Z)

R = D_BODY / 2.0
TOTAL_H = H_BODY + H_PIN


def seam(wp):
    """Turn a round feature about Z so its surface seam sits at SEAM_ANGLE."""
    return wp.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# ---------------- main body with two flats ----------------
body = seam(cq.Workplane("XY").circle(R).extrude(H_BODY))

cut_w = R - ACROSS_FLATS / 2.0 + 1.0
for sx in (1, -1):
    flat_cut = (
        cq.Workplane("XY")
        .center(sx * (ACROSS_FLATS / 2.0 + cut_w / 2.0), 0)
        .rect(cut_w, D_BODY + 2.0)
        .extrude(H_FLAT)
    )
    body = body.cut(flat_cut)

# small chamfer all round the bottom outline (arcs and flat edges)
body = body.faces("<Z").edges().chamfer(BOTTOM_CHAMFER)

# ---------------- top spigot ----------------
pin = seam(
    cq.Workplane("XY", origin=(0, 0, H_BODY))
    .circle(D_PIN / 2.0)
    .extrude(H_PIN)
    .faces(">Z")
    .edges()
    .chamfer(PIN_CHAMFER)
)
body = body.union(pin)

# ---------------- axial through hole with top countersink ----------------
thru = seam(
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .circle(D_THRU / 2.0)
    .extrude(TOTAL_H + 2.0)
)
body = body.cut(thru)

top_csk = cq.Solid.makeCone(
    D_THRU / 2.0 - 0.01,
    D_THRU / 2.0 + THRU_CHAMFER + 0.6,
    THRU_CHAMFER + 0.61,
    pnt=cq.Vector(0, 0, TOTAL_H - THRU_CHAMFER - 0.01),
    dir=cq.Vector(0, 0, 1),
)
body = body.cut(seam(cq.Workplane().add(top_csk)))

# ---------------- bottom bore with entry chamfer ----------------
bore = seam(
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .circle(D_BORE / 2.0)
    .extrude(BORE_DEPTH + 1.0)
)
body = body.cut(bore)

bore_csk = cq.Solid.makeCone(
    D_BORE / 2.0 + BORE_CHAMFER + 0.6,
    D_BORE / 2.0 - 0.01,
    BORE_CHAMFER + 0.61,
    pnt=cq.Vector(0, 0, -0.6),
    dir=cq.Vector(0, 0, 1),
)
body = body.cut(seam(cq.Workplane().add(bore_csk)))

# ---------------- set-screw cross hole from the -X flat ----------------
cross = (
    cq.Workplane("YZ", origin=(-R - 1.0, 0, Z_CROSS))
    .circle(D_CROSS / 2.0)
    .extrude(R + 1.0 - D_BORE / 4.0)   # stops inside the bore
)
body = body.cut(cross)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
